import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.GeomAPI import GeomAPI_ProjectPointOnCurve
from OCP.gp import gp_Pnt

# =====================================================================
#  S-shaped duct / hose fitting: a horizontal socket tube at the front,
#  an S-neck rising into a domed vertical cylinder at the back.
#  Y = length direction (front socket face at Y = 0), Z = up.
# =====================================================================

# ---------------- front tube ----------------
R_TUBE = 25.0          # front horizontal tube radius (tube axis = Y axis, Z = 0)
TOP_END = 33.6         # where the straight tube ends on its top line
TUBE_TILT = 0.3831       # tan of the tilt of the tube/neck joint plane (bottom line ends further back)
COLLAR_LEN = 7.0       # front collar band length
COLLAR_STEP = 0.2      # collar radial step
LIP_RO = 20.8          # protruding lip ring outer radius
LIP_RI = 19.9          # lip ring inner radius (= socket bore radius)
LIP_H = 1.3            # lip protrusion ahead of the front face
BORE_DEPTH = 6.0       # depth of the front socket recess

# ---------------- vertical cylinder + dome ----------------
CYL_Y = 102.0          # Y position of the vertical cylinder axis
R_CYL = 27.2           # vertical cylinder radius
CYL_Z0 = -0.5          # bottom of the vertical cylinder
CYL_Z1 = 28.4          # top of the vertical cylinder (dome equator)
DOME_H = 21.1          # dome height above the equator
BOT_CHAMFER = 0.8      # chamfer on the bottom rim
CYL_GAP = 0.15         # the cylinder stands proud of the dome/neck by this much (equator ledge)

# ---------------- S-neck (multi-section sweep) ----------------
# spline centre line way points (Y, Z) between the tube joint and the dome centre
NECK_WAY = [(56.41, 4.42), (82.78, 22.64)]
# intermediate sections: (path parameter, half width, upper half height, lower half height)
# (lower halves get squarer towards the cylinder: NECK_SQ per section incl. the end section)
NECK_SECS = [
    (0.3079, 22.28, 24.71, 4.33),
    (0.6427, 24.65, 20.48, 7.63),
    (0.9242, R_CYL, 21.06, 18.11),
]
PATH_SAMPLES = 7       # centre line re-sampling (surface smoothness only)
NECK_SQ = [0.72, 0.78, 0.74, 0.72]
NECK_END_LOW = 12.08    # lower half height of the end section (inside the cylinder)

# ---------------- vent hole ----------------
VENT_D = 1.8
VENT_X = -11.3
VENT_Y = 119.0
VENT_DEPTH = 5.0

VIEW = {"azimuth": 45, "elevation": 26}

X_AX = cq.Vector(1, 0, 0)
Y_AX = cq.Vector(0, 1, 0)
Z_AX = cq.Vector(0, 0, 1)


def y_circle_solid(r, y0, y1, seam_rot=130):
    """cylinder on the Y axis from y0 to y1 (seam turned to the lower -X side, seen by no view)"""
    s = cq.Workplane("XZ", origin=(0, y0, 0)).circle(r).extrude(-(y1 - y0))
    return s.rotate((0, 0, 0), (0, 1, 0), seam_rot)


def egg(c, n, w, ht, hb, sq=None):
    """closed section: upper half ellipse (height ht) + lower half (height hb).
    sq=None -> exact half ellipse below, otherwise a smooth 'squarish' curve whose
    45-degree points are pushed out to (sq*w, sq*hb) (0.707 = ellipse, ->1 = box)"""
    xd = cq.Vector(-1, 0, 0)       # with this x dir the local y axis points up
    up = cq.Edge.makeEllipse(w, ht, pnt=c, dir=n, xdir=xd, angle1=0, angle2=180)
    if sq is None:
        lo = cq.Edge.makeEllipse(w, hb, pnt=c, dir=n, xdir=xd, angle1=180, angle2=360)
        return [up, lo]
    ey = n.normalized().cross(xd).normalized()     # local up
    lo = cq.Edge.makeSpline(
        [
            c + X_AX * w,
            c + X_AX * (sq * w) - ey * (sq * hb),
            c - ey * hb,
            c - X_AX * (sq * w) - ey * (sq * hb),
            c - X_AX * w,
        ],
        tangents=[-ey, ey],
    )
    return [up, lo]


# ---------------- front tube, cut by the tilted joint plane ----------------
tilt_a = math.atan(TUBE_TILT)
JOINT_Y = TOP_END + R_TUBE * TUBE_TILT           # joint plane centre on the tube axis
joint_n = cq.Vector(0, math.cos(tilt_a), math.sin(tilt_a))

tube = y_circle_solid(R_TUBE, 0.0, JOINT_Y + R_TUBE * TUBE_TILT + 5.0)
cutter = (
    cq.Workplane("XY")
    .box(300, 300, 300, centered=(True, False, True))
    .rotate((0, 0, 0), (1, 0, 0), math.degrees(tilt_a))
    .translate((0, JOINT_Y, 0))
)
tube = tube.cut(cutter)
collar = y_circle_solid(R_TUBE + COLLAR_STEP, 0.0, COLLAR_LEN)
lip = y_circle_solid(LIP_RO, -LIP_H, 0.0)      # the socket bore below opens it up
body = tube.union(collar).union(lip)

# ---------------- vertical cylinder + elliptical dome ----------------
c0 = cq.Vector(0, CYL_Y, CYL_Z0)
c1 = cq.Vector(0, CYL_Y, CYL_Z1)
ctop = cq.Vector(0, CYL_Y, CYL_Z1 + DOME_H)
p_eq = c1 + cq.Vector(R_CYL, 0, 0)

# dome meridian: one symmetric smooth spline over the top (-X equator -> top -> +X equator)
N_ARC = 12
dome_pts = [
    c1 + cq.Vector(-R_CYL * math.cos(math.pi * i / N_ARC), 0, DOME_H * math.sin(math.pi * i / N_ARC))
    for i in range(N_ARC + 1)
]
dome_full = cq.Edge.makeSpline(dome_pts, tangents=[Z_AX, -Z_AX], scale=False)
_crv = BRep_Tool.Curve_s(dome_full.wrapped, 0.0, 1.0)
_u0, _u1 = dome_full._bounds()
_umid = GeomAPI_ProjectPointOnCurve(gp_Pnt(ctop.x, ctop.y, ctop.z), _crv).LowerDistanceParameter()
dome_right = cq.Edge(BRepBuilderAPI_MakeEdge(_crv, _umid, _u1).Edge())   # top -> +X equator

# full vertical cylinder below the dome equator (bottom rim chamfered)
# (profile drawn towards -Y so the revolve seam sits at the front, hidden under the neck)
R_CYL_OUT = R_CYL + CYL_GAP
p_b0 = c0 + cq.Vector(0, -(R_CYL_OUT - BOT_CHAMFER), 0)
p_b1 = c0 + cq.Vector(0, -R_CYL_OUT, BOT_CHAMFER)
p_fr = c1 + cq.Vector(0, -R_CYL_OUT, 0)
cyl_prof = cq.Wire.assembleEdges([
    cq.Edge.makeLine(c0, p_b0),
    cq.Edge.makeLine(p_b0, p_b1),
    cq.Edge.makeLine(p_b1, p_fr),
    cq.Edge.makeLine(p_fr, c1),
    cq.Edge.makeLine(c1, c0),
])
cyl = cq.Solid.revolve(cq.Face.makeFromWires(cyl_prof), 360, c0, c1)

# back half of the dome (Y >= CYL_Y); its front half is formed by the neck sweep
dome_prof = cq.Wire.assembleEdges([
    cq.Edge.makeLine(c1, p_eq),
    dome_right,
    cq.Edge.makeLine(ctop, c1),
])
back = cq.Solid.revolve(cq.Face.makeFromWires(dome_prof), 180, c1, ctop)

# ---------------- S-shaped neck: multi-section sweep ----------------
path_pts = [cq.Vector(0, JOINT_Y, 0)] + [cq.Vector(0, y, z) for (y, z) in NECK_WAY] + [c1]
path_e = cq.Edge.makeSpline(path_pts, tangents=[Y_AX, Y_AX])
# re-interpolate the same centre line through evenly spaced points: more spline spans along
# the path give the swept surface a finer knot grid (smoother tessellation), same shape
path_e = cq.Edge.makeSpline(
    [path_e.positionAt(i / (PATH_SAMPLES - 1)) for i in range(PATH_SAMPLES)], tangents=[Y_AX, Y_AX]
)
path_w = cq.Wire.assembleEdges([path_e])

ca = math.cos(tilt_a)
# first section = the tube cut by the joint plane (an ellipse)
secs = [cq.Wire.assembleEdges(egg(cq.Vector(0, JOINT_Y, 0), joint_n, R_TUBE, R_TUBE / ca, R_TUBE / ca))]
for (t, w, ht, hb), sq in zip(NECK_SECS, NECK_SQ):
    secs.append(cq.Wire.assembleEdges(egg(path_e.positionAt(t), path_e.tangentAt(t), w, ht, hb, sq)))
# last section: the dome meridian on top, lower half buried in the cylinder
end_sec = egg(c1, Y_AX, R_CYL, DOME_H, NECK_END_LOW, NECK_SQ[-1])
end_sec[0] = dome_full
secs.append(cq.Wire.assembleEdges(end_sec))

neck = cq.Solid.sweep_multi(secs, path_w, makeSolid=True, isFrenet=False)

body = (
    body.union(cq.Workplane().add(neck))
    .union(cq.Workplane().add(cyl))
    .union(cq.Workplane().add(back))
)

# ---------------- front socket recess ----------------
body = body.cut(y_circle_solid(LIP_RI, -LIP_H - 1.0, BORE_DEPTH, seam_rot=0))

# ---------------- small vent hole in the dome ----------------
r2 = (VENT_X ** 2 + (VENT_Y - CYL_Y) ** 2) / R_CYL ** 2
z_top = CYL_Z1 + DOME_H * math.sqrt(max(0.0, 1 - r2))
vent = (
    cq.Workplane("XY", origin=(VENT_X, VENT_Y, z_top - VENT_DEPTH))
    .circle(VENT_D / 2)
    .extrude(VENT_DEPTH + 5)
)
body = body.cut(vent)

result = body
